import math
import cadquery as cq

# ---------------------------------------------------------------------------
# "XYZ" trick cube: reads X from the sides, Y from the front / back and Z from
# the top / bottom.  The X prism (extruded along X) is the base body; its two
# V-channels (top / bottom) are filled with the Z prism and its two side
# wedges (front / back) are filled with the Y prism.
# ---------------------------------------------------------------------------

# ---------------- driving dimensions (mm) ----------------
S = 40.0          # cube edge length
STROKE = 10.0     # stroke width of the X and Y letters (also the Y stem width)
ARM_A = 15.0      # an X/Y arm's outer edge runs from a cube corner to this depth at mid height
Z_BAR = 12.5      # height of the Z top / bottom bars (= arm width at the cube edge)
Z_TIP = 19.0      # how far each Z notch reaches in from its side face
EDGE_R = 0.3      # small round on every edge

H = S / 2.0
slope = H / ARM_A                                  # arm rise / run (4:3)
ARM_B = STROKE * math.hypot(1.0, slope) / slope    # arm width measured along the cube edge
APEX = (H - ARM_B) * slope                         # depth of the V between two arms
STEM = STROKE


def ctr(pts):
    """letter coordinates (0..S) -> coordinates centred on the cube"""
    return [(u - H, v - H) for (u, v) in pts]


# letter outlines in (u, v): u to the right, v up, as seen from outside the face
Y_LET = [(0, S), (ARM_B, S), (H, S - APEX), (S - ARM_B, S), (S, S), (H + STEM / 2, H),
         (H + STEM / 2, 0), (H - STEM / 2, 0), (H - STEM / 2, H)]
X_LET = [(0, S), (ARM_B, S), (H, S - APEX), (S - ARM_B, S), (S, S), (S - ARM_A, H),
         (S, 0), (S - ARM_B, 0), (H, APEX), (ARM_B, 0), (0, 0), (ARM_A, H)]
Z_LET = [(0, 0), (S, 0), (S, Z_BAR), (S - Z_TIP, Z_BAR), (S, S - Z_BAR), (S, S),
         (0, S), (0, S - Z_BAR), (Z_TIP, S - Z_BAR), (0, Z_BAR)]

# the four notches of the X (u -> +y, v -> +z): top / bottom V channels, front / back wedges
TOP_V = [(ARM_B, S), (H, S - APEX), (S - ARM_B, S)]
BOT_V = [(ARM_B, 0), (S - ARM_B, 0), (H, APEX)]
FRONT_W = [(0, 0), (ARM_A, H), (0, S)]
BACK_W = [(S, 0), (S, S), (S - ARM_A, H)]


def prism_x(pts):   # profile in the YZ plane, extruded through the cube along X
    return cq.Workplane("YZ", origin=(-H, 0, 0)).polyline(ctr(pts)).close().extrude(S)


def prism_y(pts):   # profile in the XZ plane, extruded through the cube along Y
    return cq.Workplane("XZ", origin=(0, H, 0)).polyline(ctr(pts)).close().extrude(S)


def prism_z(pts):   # profile in the XY plane, extruded through the cube along Z
    return cq.Workplane("XY", origin=(0, 0, -H)).polyline(ctr(pts)).close().extrude(S)


x_body = prism_x(X_LET)                 # X read from the left / right
y_body = prism_y(Y_LET)                 # Y read from the front / back
z_top = prism_z(Z_LET)                  # Z read from above
z_bot = z_top.mirror("XZ")              # Z read from below

top_ch = prism_x(TOP_V)
bot_ch = prism_x(BOT_V)
side_w = prism_x(FRONT_W).union(prism_x(BACK_W))

body = (x_body
        .union(z_top.intersect(top_ch))
        .union(z_bot.intersect(bot_ch))
        .union(y_body.intersect(side_w))
        .clean())

# small round on every edge (fall back to a smaller round, then to sharp edges, if OCC refuses)
result = body
for _r in (EDGE_R, 0.5 * EDGE_R):
    try:
        _f = body.edges().fillet(_r)
        if _f.val().isValid():
            result = _f
            break
    except Exception:
        pass
